import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_L = 100.0      # flange length (X)
PLATE_W = 22.0       # flange width (Y)
PLATE_T = 9.0        # flange thickness
PLATE_R = 4.0        # flange corner radius (vertical edges)

BLOCK_X0 = -28.0     # lower block extent in X
BLOCK_X1 = 30.0
BLOCK_H = 15.5       # lower block height below the flange
BLOCK_BACK_INSET = 1.0

HOLE_PITCH = 80.0    # hole spacing
HOLE_D = 7.2         # through hole
CBORE_D = 11.8       # counterbore
CBORE_DEPTH = 4.5

POCKET_DEPTH = 0.8   # shallow recesses in the block underside
POCKET_MARGIN = 1.5
POCKET_RIB = 1.2
POCKET_SMALL = 9.6 

ARM_X = -5.6         # spout centre plane at the flange (offset from the flange centre)
ARM_X_TIP = -6.6     # spout centre at the tip (the spout leans slightly to -X)
WALL = 2.1           # wall of the hollow spout
CORNER_FRAC = 0.42   # corner radius of the spout section / its smaller side
SHOULDER_R = 3.0     # round where the spout back meets its upper surface
ROOT_R = 3.0         # blend between spout and flange top
CAVITY_FROM = 2      # index of the first path station that is hollow

Z_TOP = BLOCK_H + PLATE_T   # top of the flange
Y_BACK = PLATE_W / 2        # back face of the flange (spout is trimmed flush)

# spout centre line in the YZ plane (first point buried in the flange, last one past the tip)
CENTRE = [(12.4, 14.6), (-2.0, 29.5), (-16.1, 40.1), (-29.5, 49.3), (-44.1, 57.2), (-58.0, 63.5)]
N_STATIONS = 6
# spout thickness (perpendicular to the centre line) against the Y of the station
THICK = [(12.4, 14.2), (-2.0, 17.5), (-9.7, 17.3), (-16.1, 16.9), (-22.7, 16.0),
         (-29.5, 14.65), (-36.6, 13.4), (-44.1, 11.8), (-50.0, 10.7), (-58.0, 9.5)]
# spout width along X: linear taper with Y
W_AT_BACK, W_AT_TIP, Y_W_BACK, Y_W_TIP = 30.7, 21.0, 11.0, -50.0
# oblique cut that forms the open tip: centre and angle of its normal above -Y
TIP_C = (-49.95, 59.95)
TIP_ANG = 36.8


def interp(x, table):
    pts = sorted(table)
    if x <= pts[0][0]:
        return pts[0][1]
    for (x0, y0), (x1, y1) in zip(pts, pts[1:]):
        if x <= x1:
            return y0 + (y1 - y0) * (x - x0) / (x1 - x0)
    return pts[-1][1]


def x_at(y):
    return ARM_X + (ARM_X_TIP - ARM_X) * (Y_W_BACK - y) / (Y_W_BACK - Y_W_TIP)


def width_at(y):
    return W_AT_TIP + (W_AT_BACK - W_AT_TIP) * (y - Y_W_TIP) / (Y_W_BACK - Y_W_TIP)


def rr_wire(w, t, origin, normal, inset=0.0):
    """rounded-rectangle section; inset > 0 gives the concentric inner outline."""
    r = min(w, t) * CORNER_FRAC - inset
    w, t = w - 2 * inset, t - 2 * inset
    sk = cq.Sketch().rect(w, t).vertices().fillet(r)
    wire = sk._faces.Faces()[0].outerWire()
    pl = cq.Plane(origin=origin, xDir=(1, 0, 0), normal=normal)
    return wire.moved(cq.Location(pl))


# ---------------- base: flange + block ----------------
plate = (
    cq.Workplane("XY").workplane(offset=BLOCK_H)
    .rect(PLATE_L, PLATE_W).extrude(PLATE_T)
    .edges("|Z").fillet(PLATE_R)
)
block_w = PLATE_W - BLOCK_BACK_INSET
yc_block = -PLATE_W / 2 + block_w / 2
block = (
    cq.Workplane("XY")
    .center((BLOCK_X0 + BLOCK_X1) / 2, yc_block)
    .rect(BLOCK_X1 - BLOCK_X0, block_w).extrude(BLOCK_H + 0.5)
)
base = plate.union(block)

# ---------------- curved spout: loft of sections normal to a spline centre line ----------------
path = cq.Edge.makeSpline([cq.Vector(ARM_X, y, z) for y, z in CENTRE])
stations = []
for i in range(N_STATIONS):
    u = i / (N_STATIONS - 1)
    p = path.positionAt(u)
    tg = path.tangentAt(u)
    p = cq.Vector(x_at(p.y), p.y, p.z)
    stations.append((p, tg, width_at(p.y), interp(p.y, THICK)))

outer = [rr_wire(w, t, p.toTuple(), tg.toTuple()) for p, tg, w, t in stations]
tube = cq.Workplane().add(cq.Solid.makeLoft(outer, ruled=False))

# open tip: oblique planar cut
ca = math.radians(TIP_ANG)
tip_n = cq.Vector(0, -math.cos(ca), math.sin(ca))
tip_plane = cq.Plane(origin=(x_at(TIP_C[0]), TIP_C[0], TIP_C[1]), xDir=(1, 0, 0), normal=tip_n.toTuple())
tip_cut = cq.Workplane(tip_plane).rect(200, 200).extrude(100)
tube = tube.cut(tip_cut)

# keep only what stands above the flange (the rest is buried anyway)
low_cut = cq.Workplane("XY").box(300, 300, 100, centered=(True, True, False)).translate((0, 0, Z_TOP - 2 - 100))
tube = tube.cut(low_cut)

# trim flush with the flange back face, then round the shoulder where the flat back turns
# into the upper surface of the spout
back_cut = cq.Workplane("XY").box(300, 100, 300, centered=(True, False, True)).translate((0, Y_BACK, 0))
tube = tube.cut(back_cut)
SHOULDER_OK = None
back_face = tube.faces(cq.selectors.NearestToPointSelector((ARM_X, Y_BACK + 5, Z_TOP + 4))).val()
sh = [e for e in back_face.Edges() if e.Center().z > Z_TOP + 1]
for r in (SHOULDER_R, SHOULDER_R + 0.5, SHOULDER_R - 0.5, SHOULDER_R - 1.0, SHOULDER_R + 1.0):
    try:
        tube = tube.newObject(sh).fillet(r)
        SHOULDER_OK = r
        break
    except Exception:
        pass

# temporary pad so the root blend runs round a closed loop on a wide flat face
pad = (cq.Workplane("XY").box(50, 56, 2, centered=(True, True, False))
       .translate((ARM_X, 2.0, Z_TOP - 2)))
arm = pad.union(tube)
root = [e for e in arm.edges().vals()
        if abs(e.BoundingBox().zmin - Z_TOP) < 0.05 and abs(e.BoundingBox().zmax - Z_TOP) < 0.05
        and e.BoundingBox().xmin > ARM_X - 24 and e.BoundingBox().xmax < ARM_X + 24]
ROOT_USED = None
for r in (ROOT_R, 3.5, 2.5, 4.0, 2.0):
    try:
        arm = arm.newObject(root).fillet(r)
        ROOT_USED = r
        break
    except Exception:
        pass

# keep the blended root only between the flange faces; in front of the flange the plain spout continues
keep = (cq.Workplane("XY").box(300, PLATE_W, 300, centered=(True, False, True))
        .translate((0, -PLATE_W / 2, 0)))
front = cq.Workplane("XY").box(300, 100, 300, centered=(True, False, True)).translate((0, -PLATE_W / 2 - 100, 0))
arm = arm.intersect(keep).union(tube.intersect(front))

body = base.union(arm)

# hollow bore of the spout (inner loft on the same centre line, running out through the tip)
inner = [rr_wire(w, t, p.toTuple(), tg.toTuple(), inset=WALL)
         for p, tg, w, t in stations[CAVITY_FROM:]]
cavity = cq.Solid.makeLoft(inner, ruled=False)
body = body.cut(cq.Workplane().add(cavity))

# counterbored mounting holes
for hx in (-HOLE_PITCH / 2, HOLE_PITCH / 2):
    thru = cq.Workplane("XY").center(hx, 0).circle(HOLE_D / 2).extrude(Z_TOP + 1)
    cb = (cq.Workplane("XY").workplane(offset=Z_TOP - CBORE_DEPTH)
          .center(hx, 0).circle(CBORE_D / 2).extrude(CBORE_DEPTH + 1))
    body = body.cut(thru).cut(cb)

# shallow recesses on the block underside: small, large, large, small
blen = BLOCK_X1 - BLOCK_X0
inner_len = blen - 2 * POCKET_MARGIN - 3 * POCKET_RIB
large = (inner_len - 2 * POCKET_SMALL) / 2
x = BLOCK_X0 + POCKET_MARGIN
pk_w = block_w - 2 * POCKET_MARGIN
for L in (POCKET_SMALL, large, large, POCKET_SMALL):
    cut = cq.Workplane("XY").center(x + L / 2, yc_block).rect(L, pk_w).extrude(POCKET_DEPTH)
    body = body.cut(cut)
    x += L + POCKET_RIB

result = body

